import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Face-shield headband frame (parametric)
#   X : left / right, Y : toward the front (apex of the arcs), Z : up
#   y = 0 is the plane of the open leg ends
# ---------------------------------------------------------------------------
H = 20.0          # band height
T = 2.0           # wall thickness of the bands

# outer visor band (apex + two free wings): ellipse centred on the Y axis
A_O, B_O, YC_O = 100.9, 103.3, 36.4
WING_Y_END = 75.0          # y of the free wing ends

# lower part of the main band: leaves the outer band at the split point with a
# kink and runs down into straight legs that end (rounded) on the headband legs
SPLIT_X = 51.0             # |x| where the main band branches off
SPLIT_ANGLE = 36.0         # deg, kink between outer band and main band
MAIN_PTS = [(68.0, 107.6), (76.0, 92.8), (82.8, 75.2)]   # centre-line through points
A_M = 85.6                 # |x| of the straight main-band legs
Y_LEG_TOP = 58.0           # main band becomes straight below this y
Y_JUNCT = 40.2             # outer face of the main-band leg ends here ...
END_ROUND_L = 1.8          # ... and rounds off (elliptical foot) over this length
FOOT_RX = 2.6              # x-radius of the rounded foot (dives into the headband leg)
FOOT_Y_IN = 42.5           # inner face of the main-band leg ends here
FOOT_P = (83.0, 41.5)      # foot corner inside the headband leg

# inner headband: ellipse top + straight legs down to y = 0
A_H, B_H, YC_H = 85.6, 75.5, 25.0

END_CHAMFER = 5.0          # 45 deg chamfers on top/bottom corners of free ends

# spacers
SPACER_T = 1.5
SPACER_WING_Y = 106.0      # wing <-> main band (normal to the bands)
SPACER_HEAD_Y = 52.9       # headband <-> main band (along x)

# visor pins
PIN_R = 2.45
PIN_Z = 2.6
PIN_TIP_FILLET = 1.0
PIN_TOP_X = 29.5           # front pins, pointing +Y
PIN_TOP_TIP = 142.4
PIN_SIDE_Y = 86.8          # side pins on the wings, pointing +-X
PIN_SIDE_TIP = 95.6
PIN_SLOT_W = 1.3           # split slot in the pin head
PIN_SLOT_L = 3.6

# engraved material marking on the left main-band leg
TEXT = "PLA"
TEXT_SIZE = 10.0
TEXT_SQUEEZE = 0.62        # condensed lettering
TEXT_SLANT = 0.2           # italic shear
TEXT_Y, TEXT_Z = 53.5, 10.0
TEXT_DEPTH = 0.4

# elastic strap clips on the outer face of the leg ends
CLIP_Y0, CLIP_Y1 = 1.5, 22.8       # cap length along the leg
STEM_Y0, STEM_Y1 = 7.7, 16.9       # stem joining cap to leg
CLIP_CAP_X1 = 94.4                 # outermost x of the cap
CLIP_CAP_T = 4.9                   # cap thickness (x)
CLIP_BAR_Z0, CLIP_BAR_Z1 = 10.0, 15.0
CLIP_WEB_Z0 = 1.6
CLIP_WEB_BOT_Y0, CLIP_WEB_BOT_Y1 = 6.7, 17.5
CLIP_BAR_FILLET = 1.2
CLIP_SCOOP_R = 2.6
CLIP_SCOOP_D = 0.9


# ---------------------------------------------------------------------------
def V(x, y, z=0.0):
    return cq.Vector(x, y, z)


def unit(x, y):
    m = math.hypot(x, y)
    return (x / m, y / m)


def ell_pt(a, b, yc, t):
    return (a * math.cos(t), yc + b * math.sin(t))


def ell_normal(a, b, t):
    return unit(math.cos(t) / a, math.sin(t) / b)


def t_at_y(b, yc, y):
    return math.asin(max(-1.0, min(1.0, (y - yc) / b)))


def eo_y(x):
    return YC_O + B_O * math.sqrt(1 - (x / A_O) ** 2)


def spline(pts, t0=None, t1=None):
    vs = [V(x, y) for x, y in pts]
    if t0 is not None:
        return cq.Edge.makeSpline(vs, tangents=[V(*t0), V(*t1)])
    return cq.Edge.makeSpline(vs)


def face_prism(edges, h=H):
    f = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Solid.extrudeLinear(f, V(0, 0, h))


def band_from_samples(samples, t, cap0="line", cap1="line"):
    """samples: list of (point, unit normal) along a centre line.
    Builds a band of thickness t with one smooth spline per side."""
    outer = [(p[0] + n[0] * t / 2, p[1] + n[1] * t / 2) for p, n in samples]
    inner = [(p[0] - n[0] * t / 2, p[1] - n[1] * t / 2) for p, n in samples]
    # end tangents: normal rotated by 90 deg, oriented along the direction of travel
    n0, n1 = samples[0][1], samples[-1][1]
    chord0 = (samples[1][0][0] - samples[0][0][0], samples[1][0][1] - samples[0][0][1])
    chord1 = (samples[-1][0][0] - samples[-2][0][0], samples[-1][0][1] - samples[-2][0][1])
    tg0 = (-n0[1], n0[0])
    if tg0[0] * chord0[0] + tg0[1] * chord0[1] < 0:
        tg0 = (-tg0[0], -tg0[1])
    tg1 = (-n1[1], n1[0])
    if tg1[0] * chord1[0] + tg1[1] * chord1[1] < 0:
        tg1 = (-tg1[0], -tg1[1])
    e_out = spline(outer, tg0, tg1)
    e_in = spline(inner, tg0, tg1)
    edges = [e_out]

    def cap(pa, pb, centre, tg, kind, sgn):
        if kind == "round":
            mid = (centre[0] + sgn * tg[0] * t / 2, centre[1] + sgn * tg[1] * t / 2)
            return cq.Edge.makeThreePointArc(V(*pa), V(*mid), V(*pb))
        return cq.Edge.makeLine(V(*pa), V(*pb))

    edges.append(cap(outer[-1], inner[-1], samples[-1][0], tg1, cap1, 1.0))
    edges.append(e_in)
    edges.append(cap(inner[0], outer[0], samples[0][0], tg0, cap0, -1.0))
    return face_prism(edges)


def arch_samples(a, b, yc, y_end, n_ell=48, leg_step=5.0):
    """centre line: right leg (bottom->top), ellipse top half, left leg (top->bottom)"""
    s = []
    n_leg = max(2, int(math.ceil((yc - y_end) / leg_step)))
    for i in range(n_leg):
        s.append(((a, y_end + (yc - y_end) * i / n_leg), (1.0, 0.0)))
    for i in range(n_ell + 1):
        tt = math.pi * i / n_ell
        s.append((ell_pt(a, b, yc, tt), ell_normal(a, b, tt)))
    for i in range(1, n_leg + 1):
        s.append(((-a, yc - (yc - y_end) * i / n_leg), (-1.0, 0.0)))
    return s


# ---------------------------------------------------------------------------
def outer_samples(n=60):
    t0 = t_at_y(B_O, YC_O, WING_Y_END)
    t1 = math.pi - t0
    return [(ell_pt(A_O, B_O, YC_O, t0 + (t1 - t0) * i / n),
             ell_normal(A_O, B_O, t0 + (t1 - t0) * i / n)) for i in range(n + 1)]


def outer_band():
    return band_from_samples(outer_samples(), T)


def trim_region():
    """inside of the outer band's inner face, closed below (trims the main band)"""
    s = outer_samples()
    inner = [(p[0] - n[0] * T / 2, p[1] - n[1] * T / 2) for p, n in s]
    n0, n1 = s[0][1], s[-1][1]
    e = [spline(inner, (-n0[1], n0[0]), (-n1[1], n1[0])),
         cq.Edge.makeLine(V(*inner[-1]), V(inner[-1][0], -10)),
         cq.Edge.makeLine(V(inner[-1][0], -10), V(inner[0][0], -10)),
         cq.Edge.makeLine(V(inner[0][0], -10), V(*inner[0]))]
    return face_prism(e)


def main_centreline_right():
    xs = SPLIT_X
    ys = eo_y(xs)
    # tangent of the outer ellipse at the split, pointing away from the apex
    tt = math.acos(xs / A_O)
    d = unit(A_O * math.sin(tt), -B_O * math.cos(tt))
    be = math.radians(SPLIT_ANGLE)
    d0 = (d[0] * math.cos(-be) - d[1] * math.sin(-be), d[0] * math.sin(-be) + d[1] * math.cos(-be))
    pts = [(xs, ys)] + MAIN_PTS + [(A_M, Y_LEG_TOP)]
    return spline(pts, d0, (0.0, -1.0))


def main_band_right(n=40):
    """main band (right half): spline part from the split point, straight leg, and a
    rounded foot that dives into the headband leg (steep intersections only)"""
    sp = main_centreline_right()
    c = []
    for i in range(n + 1):
        u = i / n
        p = sp.positionAt(u)
        tg = sp.tangentAt(u)
        c.append(((p.x, p.y), unit(-tg.y, tg.x)))   # tangent rotated +90 deg -> outward
    def leg(y0, y1):
        k = max(2, int(math.ceil((y0 - y1) / 4.0)))
        return [((A_M, y0 - (y0 - y1) * i / k), (1.0, 0.0)) for i in range(1, k + 1)]
    c_out = c + leg(Y_LEG_TOP, Y_JUNCT)
    c_in = c + leg(Y_LEG_TOP, FOOT_Y_IN)
    outer = [(p[0] + nn[0] * T / 2, p[1] + nn[1] * T / 2) for p, nn in c_out]
    inner = [(p[0] - nn[0] * T / 2, p[1] - nn[1] * T / 2) for p, nn in c_in]
    n0 = c[0][1]
    tg0 = (n0[1], -n0[0])                      # direction of travel (away from split)
    e_out = spline(outer, tg0, (0.0, -1.0))
    e_in = spline(inner, tg0, (0.0, -1.0))
    xo = A_M + T / 2
    foot_c = (xo - FOOT_RX, Y_JUNCT)
    foot_b = (foot_c[0], Y_JUNCT - END_ROUND_L)
    arc = cq.Edge.makeEllipse(FOOT_RX, END_ROUND_L, V(*foot_c), V(0, 0, 1), V(1, 0, 0),
                              270.0, 360.0)
    edges = [e_out, arc,
             cq.Edge.makeLine(V(*foot_b), V(*FOOT_P)),
             cq.Edge.makeLine(V(*FOOT_P), V(*inner[-1])),
             e_in,
             cq.Edge.makeLine(V(*inner[0]), V(*outer[0]))]
    return face_prism(edges)


def wall(p0, p1, width, z0=0.0, z1=H):
    """vertical wall of given width from 2D point p0 to p1"""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    L = math.hypot(dx, dy)
    ang = math.degrees(math.atan2(dy, dx))
    b = cq.Solid.makeBox(L, width, z1 - z0, V(0, -width / 2, z0))
    b = b.rotate(V(0, 0, 0), V(0, 0, 1), ang)
    return b.translate(V(p0[0], p0[1], 0))


def ray_to_ellipse(p, d, a, b, yc):
    """smallest positive s with p + s d on the ellipse"""
    px, py = p[0], p[1] - yc
    A = (d[0] / a) ** 2 + (d[1] / b) ** 2
    B = 2 * (px * d[0] / a ** 2 + py * d[1] / b ** 2)
    C = (px / a) ** 2 + (py / b) ** 2 - 1
    disc = math.sqrt(max(0.0, B * B - 4 * A * C))
    return (-B + disc) / (2 * A)


def end_chamfer_cutters(p, tdir, ndir, c=END_CHAMFER, thick=8.0):
    """triangular prisms removing the top & bottom corners of a band end.
    p: end point on the centre line, tdir: unit tangent pointing out of the band,
    ndir: unit band normal."""
    tx, ty = tdir
    nx, ny = ndir
    out = []
    for zc, zs in ((H, -1.0), (0.0, 1.0)):
        pts = [(1.0, zc + zs * (c + 1.0)), (1.0, zc - zs * 1.0), (-c - 1.0, zc - zs * 1.0)]
        verts = [V(p[0] + tx * u - nx * thick / 2, p[1] + ty * u - ny * thick / 2, z)
                 for (u, z) in pts]
        f = cq.Face.makeFromWires(cq.Wire.makePolygon(verts, close=True))
        out.append(cq.Solid.extrudeLinear(f, V(nx * thick, ny * thick, 0)))
    return out


def pin(base_xy, d, length):
    """visor pin: cylinder with rounded tip, split by a horizontal slot; axis along 2D dir d"""
    p = cq.Workplane("YZ").circle(PIN_R).extrude(length) \
        .faces(">X").edges().fillet(PIN_TIP_FILLET)
    slot = cq.Workplane("XY").box(PIN_SLOT_L + 1.0, 2 * PIN_R + 2, PIN_SLOT_W) \
        .translate((length - (PIN_SLOT_L + 1.0) / 2 + 1.0, 0, 0))
    p = p.cut(slot).val()
    p = p.rotate(V(0, 0, 0), V(0, 0, 1), math.degrees(math.atan2(d[1], d[0])))
    p = p.translate(V(base_xy[0], base_xy[1], PIN_Z))
    return p.cut(cq.Solid.makeBox(400, 400, 10, V(-200, -200, -10)))


def clip_right():
    """strap hook on the +X leg end: stem, rounded cap bar and a tapered web under the bar"""
    x_face = A_H + T / 2 - 0.4
    x_cap0 = CLIP_CAP_X1 - CLIP_CAP_T
    stem = cq.Workplane("XY").box(x_cap0 - x_face + 0.2, STEM_Y1 - STEM_Y0,
                                  CLIP_BAR_Z1 - CLIP_WEB_Z0, centered=False) \
        .translate((x_face, STEM_Y0, CLIP_WEB_Z0))
    cap = cq.Workplane("XY").box(CLIP_CAP_T, CLIP_Y1 - CLIP_Y0,
                                 CLIP_BAR_Z1 - CLIP_BAR_Z0, centered=False) \
        .translate((x_cap0, CLIP_Y0, CLIP_BAR_Z0)) \
        .edges("|Z").fillet(CLIP_CAP_T / 2 - 0.05) \
        .faces(">Z").edges().fillet(CLIP_BAR_FILLET)
    ym = (CLIP_Y0 + CLIP_Y1) / 2
    top_w = (CLIP_Y1 - CLIP_Y0) - 1.0
    trap = cq.Workplane("YZ").polyline([
        (ym - top_w / 2, CLIP_BAR_Z0 + 0.1), (ym + top_w / 2, CLIP_BAR_Z0 + 0.1),
        (CLIP_WEB_BOT_Y1, CLIP_WEB_Z0), (CLIP_WEB_BOT_Y0, CLIP_WEB_Z0)]).close() \
        .extrude(CLIP_CAP_X1 - x_face).translate((x_face, 0, 0))
    wedge = cq.Workplane("XZ").polyline([
        (x_cap0 - 0.2, CLIP_BAR_Z0 + 0.1), (CLIP_CAP_X1 - 0.3, CLIP_BAR_Z0 + 0.1),
        (x_cap0 + 0.3, CLIP_WEB_Z0), (x_cap0 - 0.2, CLIP_WEB_Z0)]).close() \
        .extrude(-(CLIP_Y1 + 6)).translate((0, -3, 0))
    web = trap.intersect(wedge)
    clip = stem.union(cap).union(web)
    # concave saddle for the strap across the top of the stem
    zc = CLIP_BAR_Z1 + CLIP_SCOOP_R - CLIP_SCOOP_D
    scoop = cq.Workplane("XZ").center((x_face + x_cap0) / 2, zc) \
        .circle(CLIP_SCOOP_R).extrude(-(STEM_Y1 - STEM_Y0 + 1.0)) \
        .translate((0, STEM_Y0 - 0.5, 0))
    clip = clip.cut(scoop)
    return clip.val()


# ---------------------------------------------------------------------------
# bands
trim = trim_region()
mr = main_band_right()
main_low = mr.fuse(mr.mirror("YZ")).intersect(trim)
body = outer_band().fuse(main_low)
body = body.fuse(band_from_samples(arch_samples(A_H, B_H, YC_H, 0.0), T))

# spacers wing <-> main band, along the main band normal
sp_c = main_centreline_right()
u_lo, u_hi = 0.0, 1.0
for _ in range(60):                       # find parameter where centre line hits y
    um = 0.5 * (u_lo + u_hi)
    if sp_c.positionAt(um).y > SPACER_WING_Y:
        u_lo = um
    else:
        u_hi = um
pc = sp_c.positionAt(u_lo)
tc = sp_c.tangentAt(u_lo)
nc = unit(-tc.y, tc.x)
s_hit = ray_to_ellipse((pc.x, pc.y), nc, A_O, B_O, YC_O)
for sd in (1, -1):
    p0 = (sd * pc.x, pc.y)
    p1 = (sd * (pc.x + nc[0] * s_hit), pc.y + nc[1] * s_hit)
    body = body.fuse(wall(p0, p1, SPACER_T))

# spacers headband <-> main band, along x
th = t_at_y(B_H, YC_H, SPACER_HEAD_Y)
ph = ell_pt(A_H, B_H, YC_H, th)
for sd in (1, -1):
    body = body.fuse(wall((sd * ph[0], SPACER_HEAD_Y), (sd * A_M, SPACER_HEAD_Y), SPACER_T))

# chamfered free ends: leg ends (y = 0) and wing ends
t_we = t_at_y(B_O, YC_O, WING_Y_END)
pe = ell_pt(A_O, B_O, YC_O, t_we)
ne = ell_normal(A_O, B_O, t_we)
te = (ne[1], -ne[0])                       # tangent pointing down along the wing
for sd in (1, -1):
    for c in end_chamfer_cutters((sd * A_H, 0.0), (0.0, -1.0), (sd * 1.0, 0.0)):
        body = body.cut(c)
    for c in end_chamfer_cutters((sd * pe[0], pe[1]), (sd * te[0], te[1]), (sd * ne[0], ne[1])):
        body = body.cut(c)

# strap clips
clip = clip_right()
body = body.fuse(clip).fuse(clip.mirror("YZ"))

# visor pins
for sd in (1, -1):
    y_c = eo_y(PIN_TOP_X)                  # front pins (+Y) from the band centre line
    body = body.fuse(pin((sd * PIN_TOP_X, y_c), (0.0, 1.0), PIN_TOP_TIP - y_c))
    x_c = A_O * math.sqrt(1 - ((PIN_SIDE_Y - YC_O) / B_O) ** 2)   # side pins (+-X)
    body = body.fuse(pin((sd * x_c, PIN_SIDE_Y), (sd * 1.0, 0.0), PIN_SIDE_TIP - x_c))

# material marking (engraved, condensed italic text on the outer face of the left leg)
try:
    tp = cq.Plane(origin=(0, 0, 0), xDir=(0, -1, 0), normal=(-1, 0, 0))
    txt = cq.Workplane(tp).text(TEXT, TEXT_SIZE, TEXT_DEPTH + 0.3).val()
    txt = txt.transformGeometry(cq.Matrix([[1, 0, 0, 0], [0, TEXT_SQUEEZE, -TEXT_SLANT, 0],
                                            [0, 0, 1, 0]]))
    tb = txt.BoundingBox()
    txt = txt.translate(V(-(A_M + T / 2) + TEXT_DEPTH, TEXT_Y - (tb.ymin + tb.ymax) / 2,
                          TEXT_Z - (tb.zmin + tb.zmax) / 2))
    body = body.cut(txt)
except Exception:
    pass

result = cq.Workplane("XY").newObject([body.clean()])

VIEW = {"azimuth": 45, "elevation": 26}
